"""Sliding carriage / mounting block.

Rectangular block with rounded front corners, a semicircular guide groove
along each side edge of the top face (with a V-bottomed lead-in recess at
its front end), two large slightly tapered through bores, a through pocket
with an elliptical front, three M5 clearance holes with hex nut traps from
below, a small tapered notch at the top front centre and a thin slotted
tab projecting from the bottom of the front face.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 78.0          # overall width (X)
D = 40.3          # body depth (Y), without the front tab
H = 15.0          # body height (Z)
R_CORNER = 14.0   # vertical round on the two front corners

# guide grooves along Y near each X end (semicircular, centre on top face)
G_R = 2.45
G_OFF = 4.85      # groove centre distance from the side face

# V-bottomed recess at the front end of each guide groove
V_HALF = 4.2      # half width of recess (centred on the groove)
V_SIDE = 2.4      # depth of recess at its side walls
V_MID = 5.0       # depth at the centre of the V
V_LEN = 12.3      # length of recess measured from the front face

# large through bores (slight draft: wider at the top)
BIG_D_TOP = 18.3
BIG_D_BOT = 17.8
BIG_X = 18.2      # +/- X position
BIG_Y = -6.0

# small through holes with hex nut traps from below
SM_D = 4.8
SM_POS = [(-24.3, 10.1), (24.3, 10.1), (0.0, BIG_Y)]
HEX_AF = 8.4      # nut trap across flats
HEX_DEPTH = 8.0

# through pocket: rectangle at the back, half-ellipse towards the front
P_HALF = 10.35    # half width
P_BACK = 17.7     # Y of the back wall
P_SIDE_END = 7.3  # Y where the straight sides end / ellipse centre
P_ARC_LOW = 2.2   # Y of the front-most point of the ellipse

# top front centre notch (shallow half-cone along Y)
N_D_FRONT = 6.6
N_D_BACK = 6.2
N_LEN = 6.7

# front tab at the bottom
T_THK = 5.0                  # tab thickness
T_OUT = 6.6                  # protrusion beyond the front face
T_HALF = 7.4                 # half width of the straight front edge
T_LEFT = -(W / 2 - R_CORNER)  # chamfered side starts at the corner tangent
SLOT_L = 8.3
SLOT_W = 2.0
SLOT_R = 0.3
SLOT_Y = 2.75                # slot centre distance from the front face

YF = -D / 2.0     # front face
YB = D / 2.0      # back face
EPS = 1.0         # overshoot for clean through cuts
SEAM_ANGLE = 45.0 # angular position of the seam of round holes

# ---------------- main body ----------------
body = (
    cq.Workplane("XY")
    .rect(W, D)
    .extrude(H)
    .edges("|Z and <Y")
    .fillet(R_CORNER)
)

# ---------------- front tab ----------------
tab = (
    cq.Workplane("XY")
    .polyline(
        [
            (T_LEFT, YF + EPS),
            (T_LEFT, YF),
            (-T_HALF, YF - T_OUT),
            (T_HALF, YF - T_OUT),
            (T_HALF, YF + EPS),
        ]
    )
    .close()
    .extrude(T_THK)
)
body = body.union(tab)

slot = (
    cq.Workplane("XY", origin=(0, 0, -EPS))
    .center(0, YF - SLOT_Y)
    .rect(SLOT_L, SLOT_W)
    .extrude(T_THK + 2 * EPS)
    .edges("|Z")
    .fillet(SLOT_R)
)
body = body.cut(slot)

# ---------------- guide grooves + V lead-in recesses (mirrored) ----------------
for sx in (-1, 1):
    xc = sx * (W / 2 - G_OFF)
    groove = (
        cq.Workplane("XZ", origin=(xc, YB + EPS, H))
        .circle(G_R)
        .extrude(D + 2 * EPS + 10)
    )
    body = body.cut(groove)

    v_profile = [
        (xc - V_HALF, H + EPS),
        (xc - V_HALF, H - V_SIDE),
        (xc, H - V_MID),
        (xc + V_HALF, H - V_SIDE),
        (xc + V_HALF, H + EPS),
    ]
    recess = (
        cq.Workplane("XZ", origin=(0, YF + V_LEN, 0))
        .polyline(v_profile)
        .close()
        .extrude(V_LEN + 5)
    )
    body = body.cut(recess)

# ---------------- top front centre notch ----------------
n_k = (N_D_FRONT - N_D_BACK) / 2.0 / N_LEN   # radius change per mm
notch = cq.Solid.makeCone(
    N_D_FRONT / 2 + n_k * EPS,
    N_D_BACK / 2,
    N_LEN + EPS,
    cq.Vector(0, YF - EPS, H),
    cq.Vector(0, 1, 0),
)
body = body.cut(cq.Workplane("XY").add(notch))

# ---------------- large bores ----------------
big_k = (BIG_D_TOP - BIG_D_BOT) / 2.0 / H    # radius change per mm of height
for bx in (-BIG_X, BIG_X):
    bore = cq.Solid.makeCone(
        BIG_D_BOT / 2 - big_k * EPS,
        BIG_D_TOP / 2 + big_k * EPS,
        H + 2 * EPS,
        cq.Vector(bx, BIG_Y, -EPS),
        cq.Vector(0, 0, 1),
    )
    # turn the (invisible) seam line of the conical face onto the
    # 45 deg diagonal, where it lies on the silhouette in the iso views
    bore = bore.rotate(cq.Vector(bx, BIG_Y, 0), cq.Vector(bx, BIG_Y, 1), SEAM_ANGLE)
    body = body.cut(cq.Workplane("XY").add(bore))

# ---------------- small holes + hex nut traps from below ----------------
for (px, py) in SM_POS:
    hole = cq.Solid.makeCylinder(
        SM_D / 2, H + 2 * EPS, cq.Vector(px, py, -EPS), cq.Vector(0, 0, 1)
    ).rotate(cq.Vector(px, py, 0), cq.Vector(px, py, 1), SEAM_ANGLE)
    body = body.cut(cq.Workplane("XY").add(hole))

hex_ac = HEX_AF / math.cos(math.radians(30))  # across corners
nut_traps = (
    cq.Workplane("XY", origin=(0, 0, -EPS))
    .pushPoints(SM_POS)
    .polygon(6, hex_ac)
    .extrude(HEX_DEPTH + EPS)
)
body = body.cut(nut_traps)

# ---------------- through pocket ----------------
pocket_rect = (
    cq.Workplane("XY", origin=(0, 0, -EPS))
    .center(0, (P_BACK + P_SIDE_END) / 2)
    .rect(2 * P_HALF, P_BACK - P_SIDE_END)
    .extrude(H + 2 * EPS)
)
pocket_front = (
    cq.Workplane("XY", origin=(0, 0, -EPS))
    .center(0, P_SIDE_END)
    .ellipse(P_HALF, P_SIDE_END - P_ARC_LOW)
    .extrude(H + 2 * EPS)
)
body = body.cut(pocket_rect.union(pocket_front))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
